import math
import cadquery as cq

# ---------------------------------------------------------------
# Slot-car style chassis: flat plate, front axle in 4 bearing
# blocks, 4 tall body posts, tube frame, ears with stepped posts,
# rear wall and motor box.  X lateral, Y front(0) -> rear, Z up.
# ---------------------------------------------------------------

T = 1.65           # plate thickness

# front plate
FW = 57.6          # width
FL = 30.3          # length (Y)
FCR = 2.3          # corner radius

# narrow centre plate
NH = 13.3          # half width
N_Y1 = 97.7        # rear end of plate
NECK_RX, NECK_RY = 10.0, 9.2   # concave neck sweep front plate -> narrow plate
NECK_DEPTH = 4.8  # distance of neck arc middle from the inner corner
BULGE_X = 14.9     # side bulge max half width
BULGE_Y = (38.3, 57.0)

# ears
EAR_Y = 75.0
EAR_POST_X = 15.8
EAR_HOLE_X = 22.0
EAR_R = 2.9
EAR_SPAN = 9.8     # half length of ear root along plate edge

# flexure strips along concave edges (openings behind them)
SLOT_STRIP = 0.9
NECK_HOLE = 5.4    # reach of the neck opening along the plate edges
PAD_R = 3.5        # solid pad around the ear post
BRIDGE_HW = 2.0    # half width of bridge between ear pad and lobe

# L-shaped cut-out in front plate
CUT_LO = (-4.5, 10.45, 0.95, 18.3)    # x0, x1, y0, y1
CUT_HI = (5.2, 10.45, 18.3, 36.6)

# window with raised frame
WIN_W, WIN_L, WIN_YC = 8.0, 14.4, 79.8
FRAME_W, FRAME_L, FRAME_YC, FRAME_H = 12.8, 19.5, 79.45, 1.9
FRAME_HOLE_YS = (71.15, 88.15)
FRAME_R = 1.4      # rounded outer top edges of the frame

# front axle / bearings
AX_Y, AX_Z = 7.2, 4.25
AX_HEX_F = 2.3    # hex bar across flats (corners up/down)
AX_X0, AX_X1 = -52.4, 43.0
PIN_D, PIN_L = 1.6, 5.5
BRG_XS = (-27.7, -5.8, 12.0, 27.7)
BRG_Y = 10.1
BRG_R = 5.7
BRG_T = 2.5
BRG_HOLE_D = 2.9
BRG_HOLE_Z = 4.05

# tall body posts
POST_XS = (-22.3, 22.3)
POST_YS = (4.0, 18.9)
POST_D = 3.4
POST_TOP = 17.9
DOME_R, DOME_H = 3.1, 3.5   # half-ellipsoid post foot
POST_HOLE_D = 1.2

# ear posts (stepped)
EPOST_D = 4.9
EPOST_TOP = 10.0
EPIN_D = 1.7
EPIN_TOP = 11.5
EPOST_FLARE = (1.0, 2.4)   # concave foot (horizontal, vertical)

# tube frame
ROD_D = 3.0
ROD_X = 11.6
ROD_Z = T + 0.1
ROD_Y_FRONT = 0.15
ROD_A_END = 22.5
ROD_B_START = 31.0
ROD_Y_REAR = 91.3
ROD_BEND = 2.6

# rear: cross beam, wall, box
BEAM_Y0, BEAM_Y1, BEAM_H = 91.9, 97.7, 1.8
WALL_W, WALL_T, WALL_TOP = 22.8, 2.5, 21.5
WALL_Y = 93.6
WALL_TILT = 3.0
BOX_W = 20.6
BOX_Y0, BOX_Y1 = 96.3, 118.7
BOX_Z0, BOX_Z1 = -4.8, 7.4
GUS_X1 = 13.15
GUS_Y0, GUS_Y1 = 95.9, 113.7
GUS_TOP, GUS_TOP_REAR = 9.6, 5.0
GUS_XI = 8.3       # inner end of gusset top slope at the wall
GUS_BOT = 0.3
GUS_MID = 3.6      # crease between lower and upper gusset part
GUS_LEAN = 0.6     # inward lean of the upper gusset face

# transverse ribs
RIBS = ((38.3, 0.5, 1), (55.7, 0.0, -1))   # (y, x centre, facing)
RIB_L, RIB_W, RIB_H, RIB_TOP = 12.4, 2.7, 2.2, 0.7


def box(x0, x1, y0, y1, z0, z1):
    return (cq.Workplane("XY")
            .box(x1 - x0, y1 - y0, z1 - z0, centered=False)
            .translate((x0, y0, z0)))


def cyl_z(x, y, z0, h, d):
    return cq.Workplane("XY").workplane(offset=z0).center(x, y).circle(d / 2).extrude(h)


def circle3(p1, p2, p3):
    ax, ay = p1
    bx, by = p2
    cx, cy = p3
    d = 2 * (ax * (by - cy) + bx * (cy - ay) + cx * (ay - by))
    ux = ((ax * ax + ay * ay) * (by - cy) + (bx * bx + by * by) * (cy - ay) + (cx * cx + cy * cy) * (ay - by)) / d
    uy = ((ax * ax + ay * ay) * (cx - bx) + (bx * bx + by * by) * (ax - cx) + (cx * cx + cy * cy) * (bx - ax)) / d
    return (ux, uy), math.hypot(ax - ux, ay - uy)


def flex_hole(p_a, p_m, p_b, region, strip):
    """Opening behind a concave plate edge (arc through p_a, p_m, p_b):
    only a thin flexure strip of width `strip` is left along the edge."""
    (cx, cy), r = circle3(p_a, p_m, p_b)
    return region.cut(cyl_z(cx, cy, -2, T + 4, 2 * (r + strip)))


# ---------------- plate outline (right half, mirrored) ----------------
c45 = math.cos(math.radians(45))
neck_a = (NH + NECK_RX, FL)
neck_m = (NH + NECK_DEPTH * c45, FL + NECK_DEPTH * c45)
neck_b = (NH, FL + NECK_RY)

lobe_ang = math.radians(72)
lobe_lo = (EAR_HOLE_X - EAR_R * math.cos(lobe_ang), EAR_Y - EAR_R * math.sin(lobe_ang))
lobe_hi = (EAR_HOLE_X - EAR_R * math.cos(lobe_ang), EAR_Y + EAR_R * math.sin(lobe_ang))
lobe_tip = (EAR_HOLE_X + EAR_R, EAR_Y)
ear_lo_root = (NH, EAR_Y - EAR_SPAN)
ear_hi_root = (NH, EAR_Y + EAR_SPAN)


def concave_mid(p, q, sag):
    mx, my = 0.5 * (p[0] + q[0]), 0.5 * (p[1] + q[1])
    dx, dy = q[0] - p[0], q[1] - p[1]
    ln = math.hypot(dx, dy)
    return (mx - sag * dy / ln, my + sag * dx / ln)


flank_lo_m = concave_mid(ear_lo_root, lobe_lo, 0.9)
flank_hi_m = concave_mid(lobe_hi, ear_hi_root, 0.9)

outline = (cq.Workplane("XY")
           .moveTo(0, 0)
           .lineTo(FW / 2 - FCR, 0)
           .threePointArc((FW / 2 - FCR + FCR * c45, FCR - FCR * c45), (FW / 2, FCR))
           .lineTo(FW / 2, FL - FCR)
           .threePointArc((FW / 2 - FCR + FCR * c45, FL - FCR + FCR * c45), (FW / 2 - FCR, FL))
           .lineTo(*neck_a)
           .threePointArc(neck_m, neck_b)
           .threePointArc((BULGE_X, 0.5 * (BULGE_Y[0] + BULGE_Y[1])), (NH, BULGE_Y[1]))
           .lineTo(*ear_lo_root)
           .threePointArc(flank_lo_m, lobe_lo)
           .threePointArc(lobe_tip, lobe_hi)
           .threePointArc(flank_hi_m, ear_hi_root)
           .lineTo(NH, N_Y1)
           .lineTo(0, N_Y1)
           .mirrorY())
plate = outline.extrude(T)

# flexure openings behind the concave neck and ear flank edges
holes = None
for sgn in (1, -1):
    neck_region = (box(NH, NH + NECK_RX, FL, FL + NECK_RY, -1, T + 1)
                   .intersect(cyl_z(NH, FL, -1, T + 2, 2 * NECK_HOLE)))
    h_neck = flex_hole(neck_a, neck_m, neck_b, neck_region, SLOT_STRIP)
    ear_keep = (cyl_z(EAR_POST_X, EAR_Y, -2, T + 4, 2 * PAD_R)
                .union(cyl_z(EAR_HOLE_X, EAR_Y, -2, T + 4, 2 * EAR_R))
                .union(box(EAR_POST_X, EAR_HOLE_X, EAR_Y - BRIDGE_HW, EAR_Y + BRIDGE_HW, -2, T + 2)))
    h_hi = flex_hole(lobe_hi, flank_hi_m, ear_hi_root,
                     box(NH, EAR_HOLE_X, EAR_Y, EAR_Y + EAR_SPAN, -1, T + 1), SLOT_STRIP)
    h_lo = flex_hole(ear_lo_root, flank_lo_m, lobe_lo,
                     box(NH, EAR_HOLE_X, EAR_Y - EAR_SPAN, EAR_Y, -1, T + 1), SLOT_STRIP)
    h = h_neck.union(h_hi.cut(ear_keep)).union(h_lo.cut(ear_keep))
    if sgn < 0:
        h = h.mirror("YZ")
    holes = h if holes is None else holes.union(h)
plate = plate.cut(holes)

# cut-outs
lo = box(CUT_LO[0], CUT_LO[1], CUT_LO[2], CUT_LO[3], -1, T + 1)
hi = box(CUT_HI[0], CUT_HI[1], CUT_HI[2] - 0.5, CUT_HI[3], -1, T + 1)
plate = plate.cut(lo.union(hi))
plate = plate.cut(box(-WIN_W / 2, WIN_W / 2, WIN_YC - WIN_L / 2, WIN_YC + WIN_L / 2, -1, T + 1))
for (hx, hy, hd) in [(1.3, 20.9, 1.8), (1.3, 32.0, 1.8), (-EAR_HOLE_X, EAR_Y, 1.4), (EAR_HOLE_X, EAR_Y, 1.4)]:
    plate = plate.cut(cyl_z(hx, hy, -1, T + 2, hd))

result = plate

# ---------------- window frame ----------------
fy0, fy1 = FRAME_YC - FRAME_L / 2, FRAME_YC + FRAME_L / 2
frame = box(-FRAME_W / 2, FRAME_W / 2, fy0, fy1, T - 0.01, T + FRAME_H)
frame = frame.edges("|Y").edges(">Z").fillet(FRAME_R)
frame = frame.cut(box(-WIN_W / 2, WIN_W / 2, WIN_YC - WIN_L / 2, WIN_YC + WIN_L / 2, 0, T + FRAME_H + 1))
for hy in FRAME_HOLE_YS:
    frame = frame.cut(cyl_z(0, hy, T, FRAME_H + 1, 1.1))
result = result.union(frame)

# ---------------- ribs ----------------
# two wedge shaped walls whose vertical faces look at each other
for (ry, rx, facing) in RIBS:
    y0, y1 = ry - RIB_W / 2, ry + RIB_W / 2
    if facing > 0:      # vertical face towards +Y, slope towards the front
        pts = [(y0, T - 0.01), (y1, T - 0.01), (y1, T + RIB_H), (y1 - RIB_TOP, T + RIB_H)]
    else:               # vertical face towards -Y, slope towards the rear
        pts = [(y0, T - 0.01), (y1, T - 0.01), (y0 + RIB_TOP, T + RIB_H), (y0, T + RIB_H)]
    rib = (cq.Workplane("YZ", origin=(rx - RIB_L / 2, 0, 0))
           .polyline(pts).close()
           .extrude(RIB_L))
    result = result.union(rib)

# ---------------- bearings ----------------
for bx in BRG_XS:
    b = (cq.Workplane("YZ", origin=(bx - BRG_T / 2, 0, 0))
         .moveTo(BRG_Y - BRG_R, T - 0.01)
         .threePointArc((BRG_Y, T + BRG_R), (BRG_Y + BRG_R, T - 0.01))
         .close()
         .extrude(BRG_T))
    result = result.union(b)
result = result.cut(
    cq.Workplane("YZ", origin=(-40, 0, 0)).center(BRG_Y, BRG_HOLE_Z).circle(BRG_HOLE_D / 2).extrude(80))

# ---------------- tube frame ----------------
def rod(p0, p1, d):
    v = cq.Vector(p1) - cq.Vector(p0)
    return cq.Workplane(cq.Solid.makeCylinder(d / 2, v.Length, cq.Vector(p0), v))


result = result.union(rod((-ROD_X, ROD_Y_FRONT, ROD_Z), (-ROD_X, ROD_A_END, ROD_Z), ROD_D))

path = (cq.Workplane("XY", origin=(0, 0, ROD_Z))
        .moveTo(ROD_X, ROD_Y_FRONT)
        .lineTo(ROD_X, ROD_Y_REAR - ROD_BEND)
        .threePointArc((ROD_X - ROD_BEND * (1 - c45), ROD_Y_REAR - ROD_BEND + ROD_BEND * c45),
                       (ROD_X - ROD_BEND, ROD_Y_REAR))
        .lineTo(-ROD_X + ROD_BEND, ROD_Y_REAR)
        .threePointArc((-ROD_X + ROD_BEND * (1 - c45), ROD_Y_REAR - ROD_BEND + ROD_BEND * c45),
                       (-ROD_X, ROD_Y_REAR - ROD_BEND))
        .lineTo(-ROD_X, ROD_B_START))
tube = (cq.Workplane("XZ", origin=(ROD_X, ROD_Y_FRONT, ROD_Z))
        .circle(ROD_D / 2)
        .sweep(path, transition="round"))
result = result.union(tube)

# ---------------- axle ----------------
def hex_bar(x0, x1, f):
    rc = f / math.sqrt(3)          # corner radius
    pts = [(AX_Y + rc * math.cos(math.radians(90 + 60 * i)),
            AX_Z + rc * math.sin(math.radians(90 + 60 * i))) for i in range(6)]
    return cq.Workplane("YZ", origin=(x0, 0, 0)).polyline(pts).close().extrude(x1 - x0)


result = result.union(hex_bar(AX_X0 + PIN_L, AX_X1 - PIN_L, AX_HEX_F))
result = result.union(hex_bar(AX_X1 - PIN_L, AX_X1 - PIN_L + 0.6, AX_HEX_F * 1.2))
result = result.union(rod((AX_X0, AX_Y, AX_Z), (AX_X0 + PIN_L + 0.1, AX_Y, AX_Z), PIN_D))
result = result.union(rod((AX_X1 - PIN_L - 0.1, AX_Y, AX_Z), (AX_X1, AX_Y, AX_Z), PIN_D))


# ---------------- posts ----------------
def flared_post(x, y, d, top, flare):
    r = d / 2
    a, b = flare
    prof = (cq.Workplane("XZ", origin=(x, y, 0))
            .moveTo(0, T - 0.5).lineTo(0, top).lineTo(r, top).lineTo(r, T + b)
            .threePointArc((r + a - a * c45, T + b - b * c45), (r + a, T))
            .lineTo(r + a, T - 0.5).close())
    return prof.revolve(360, (0, 0, 0), (0, 1, 0))


def dome_post(x, y, d, top, rd, hd):
    """Post with a dome shaped foot: circular arc through three points of
    a half ellipse with semi axes rd (horizontal) and hd (vertical)."""
    r = d / 2
    a1 = math.acos(r / rd)
    am = 0.5 * a1
    prof = (cq.Workplane("XZ", origin=(x, y, 0))
            .moveTo(0, T - 0.5).lineTo(rd, T - 0.5).lineTo(rd, T)
            .threePointArc((rd * math.cos(am), T + hd * math.sin(am)),
                           (r, T + hd * math.sin(a1)))
            .lineTo(r, top).lineTo(0, top).close())
    return prof.revolve(360, (0, 0, 0), (0, 1, 0))


for px in POST_XS:
    for py in POST_YS:
        p = dome_post(px, py, POST_D, POST_TOP, DOME_R, DOME_H)
        result = result.union(p)
        result = result.cut(cyl_z(px, py, POST_TOP - 3.0, 3.5, POST_HOLE_D))

for s in (-1, 1):
    p = flared_post(s * EAR_POST_X, EAR_Y, EPOST_D, EPOST_TOP, EPOST_FLARE)
    p = p.faces(">Z").edges().chamfer(0.35)
    result = result.union(p)
    result = result.union(cyl_z(s * EAR_POST_X, EAR_Y, EPOST_TOP - 0.1, EPIN_TOP - EPOST_TOP + 0.1, EPIN_D))

# ---------------- rear structure ----------------
result = result.union(box(-NH, NH, BEAM_Y0, BEAM_Y1, T - 0.01, T + BEAM_H))
wall = box(-WALL_W / 2, WALL_W / 2, -WALL_T / 2, WALL_T / 2, 0, WALL_TOP - T - BEAM_H)
wall = wall.rotate((0, 0, 0), (1, 0, 0), WALL_TILT).translate((0, WALL_Y + WALL_T / 2, T + BEAM_H - 0.2))
result = result.union(wall)

boxb = box(-BOX_W / 2, BOX_W / 2, BOX_Y0, BOX_Y1, BOX_Z0, BOX_Z1)
result = result.union(boxb)


def polyhedron(faces_pts):
    faces = [cq.Face.makeFromWires(cq.Wire.makePolygon([cq.Vector(*p) for p in pts], close=True))
             for pts in faces_pts]
    solid = cq.Solid.makeSolid(cq.Shell.makeShell(faces)).fix()
    if solid.Volume() < 0:
        solid = cq.Solid(solid.wrapped.Reversed())
    return cq.Workplane(solid)


for s in (-1, 1):
    fo_b = (s * GUS_X1, GUS_Y0, GUS_BOT)
    fo_m = (s * GUS_X1, GUS_Y0, GUS_MID)
    fo_t = (s * (GUS_X1 - GUS_LEAN), GUS_Y0, GUS_TOP)
    fi_b = (s * GUS_XI, GUS_Y0, GUS_BOT)
    fi_m = (s * GUS_XI, GUS_Y0, GUS_MID)
    fi_t = (s * GUS_XI, GUS_Y0, BOX_Z1)
    r_b = (s * BOX_W / 2, GUS_Y1, GUS_BOT)
    r_m = (s * BOX_W / 2, GUS_Y1, GUS_MID)
    r_t = (s * BOX_W / 2, GUS_Y1, GUS_TOP_REAR)
    lower = polyhedron([[fo_b, fo_m, fi_m, fi_b],
                        [fo_b, r_b, r_m, fo_m],
                        [fo_m, r_m, fi_m],
                        [fo_b, fi_b, r_b],
                        [fi_b, fi_m, r_m, r_b]])
    upper = polyhedron([[fo_m, fo_t, fi_t, fi_m],
                        [fo_m, r_m, r_t],
                        [fo_m, r_t, fo_t],
                        [fo_t, r_t, fi_t],
                        [fo_m, fi_m, r_m],
                        [fi_m, fi_t, r_t, r_m]])
    result = result.union(lower).union(upper)

VIEW = {"azimuth": 45, "elevation": 26}
